import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FLANGE_D = 40.0        # base flange diameter
FLANGE_H = 10.0        # base flange thickness
FLANGE_FILLET = 1.75   # round on the bottom outer edge of the flange
BOSS_D = 26.0          # upper cylinder diameter
BOSS_H = 21.5          # upper cylinder height above the flange
CROSS_HOLE_D = 4.9     # radial through hole (along Y)
CROSS_HOLE_Z = 10.6    # cross-hole axis height above the flange top
KEY_W = 5.8            # key block width (along Y)
KEY_H = 11.6           # key block height above the flange top

# helical wire / helical hole (right-handed helix about the part axis)
HELIX_R = 8.0          # helix centre-line radius
HELIX_PITCH = 32.0     # helix pitch
HELIX_TURNS = 2        # wire length in full turns (both ends at END_ANGLE)
END_ANGLE = 180.0      # angular position of both wire ends (deg, from +X)
TOP_CROSS_ANGLE = -63.0  # where the centre line crosses the boss top face
WIRE_D = 5.7           # wire diameter
HOLE_D = 4.8           # helical hole diameter in the plain part
END_TILT = 10.0        # extra tilt of the wire end faces (deg)
WIRE_SEAM = 270.0      # seam position around the wire section (cosmetic)
HOLE_SEAM = 0.0        # seam position around the hole section (cosmetic)

PART_SPACING = 48.5    # centre distance of the two parts (along X)

TOTAL_H = FLANGE_H + BOSS_H


def make_body():
    flange = (
        cq.Workplane("XY")
        .circle(FLANGE_D / 2.0)
        .extrude(FLANGE_H)
        .faces("<Z")
        .edges()
        .fillet(FLANGE_FILLET)
    )
    boss = (
        cq.Workplane("XY")
        .workplane(offset=FLANGE_H)
        .circle(BOSS_D / 2.0)
        .extrude(BOSS_H)
    )
    key_in = BOSS_D / 2.0 - 2.0
    key_out = FLANGE_D / 2.0
    key = (
        cq.Workplane("XY")
        .workplane(offset=FLANGE_H)
        .center((key_in + key_out) / 2.0, 0)
        .rect(key_out - key_in, KEY_W)
        .extrude(KEY_H)
    )
    body = flange.union(boss).union(key)
    # radial cross hole through the boss along Y
    cross = (
        cq.Workplane("XZ")
        .workplane(offset=-FLANGE_D)
        .center(0, FLANGE_H + CROSS_HOLE_Z)
        .circle(CROSS_HOLE_D / 2.0)
        .extrude(2 * FLANGE_D)
    )
    return body.cut(cross)


def make_helix_rod(diameter, tilt_deg, seam_deg):
    """Round rod swept along a right-handed helix of HELIX_TURNS turns.

    Both ends sit at END_ANGLE; the helix phase is chosen so that the centre
    line crosses the boss top face at TOP_CROSS_ANGLE.
    """
    height = HELIX_PITCH * HELIX_TURNS
    path = cq.Wire.makeHelix(HELIX_PITCH, height, HELIX_R)
    lam = math.atan2(HELIX_PITCH, 2 * math.pi * HELIX_R)  # lead angle
    a = lam + math.radians(tilt_deg)
    # profile plane normal: helix tangent at the start, tilted towards +Z;
    # seam_deg places the circle seam: 0 outer side, 90 top, 180 inner, 270 under
    normal = cq.Vector(0, math.cos(a), math.sin(a))
    s = math.radians(seam_deg)
    x_dir = cq.Vector(math.cos(s), -math.sin(s) * math.sin(a), math.sin(s) * math.cos(a))
    plane = cq.Plane(origin=(HELIX_R, 0, 0), xDir=x_dir, normal=normal)
    prof = cq.Workplane(plane).circle(diameter / 2.0)
    rod = prof.sweep(cq.Workplane().add(path), isFrenet=True).val()
    rod = rod.rotate((0, 0, 0), (0, 0, 1), END_ANGLE)
    # angle travelled from the lower end to the top-face crossing
    cross = (TOP_CROSS_ANGLE - END_ANGLE) % 360.0 + 360.0 * (HELIX_TURNS - 1)
    z0 = TOTAL_H - HELIX_PITCH * cross / 360.0
    return rod.translate((0, 0, z0))


wire_solid = make_helix_rod(WIRE_D, END_TILT, WIRE_SEAM)
hole_solid = make_helix_rod(HOLE_D, 0.0, HOLE_SEAM)

# left part: plain body with the empty helical hole through it
left = make_body().cut(cq.Workplane().add(hole_solid))
left = left.translate((-PART_SPACING / 2.0, 0, 0))

# right part: the same body with the helical wire threaded through it
right = make_body().union(cq.Workplane().add(wire_solid))
right = right.translate((PART_SPACING / 2.0, 0, 0))

result = cq.Workplane().add(cq.Compound.makeCompound([left.val(), right.val()]))

VIEW = {"azimuth": 45, "elevation": 26}
